import math
import cadquery as cq

# ---------------------------------------------------------------------------
# Driving dimensions (mm).  X along the beam, Y across, Z up.
# Left boss centre at X=0, right boss centre at X=BOSS_DX.
# Z=0 is the underside of the upper plate (start of the belly).
# ---------------------------------------------------------------------------
R1 = 25.7            # left boss radius
R2 = 20.9            # right boss radius
BOSS_DX = 189.0      # centre distance between the bosses

# upper plate top surface: shallow concave arc (thicker at the left end)
TOP_LOW_X = 149.0    # X of the lowest point of the top surface
TOP_LOW_Z = 7.12     # lowest height of the top surface
TOP_ARC_R = 1630.5
TOP_MAX_Z = 15.5     # plate blank height (hidden inside the left ring)

RING1_TOP = 16.0     # top of the raised ring on the left boss
RING2_TOP = 11.2     # top of the raised ring on the right boss
RECESS_D = 31.0      # shallow recess in each ring
RECESS_DEPTH = 3.5

# belly (lower curved body)
BELLY_BOTTOM = -26.0           # lowest point of the belly arc
BELLY_ARC_R = 319.0            # radius of the belly arc (axis along Y)
BELLY_ARC_CX = BOSS_DX / 2.0   # arc centre X
BELLY_DRAFT = 6.0              # side draft of the belly (deg)
BELLY_FILLET = 1.5

# bottom pockets in the bosses (cut normal to the belly arc)
POCKET1_D = 44.0
POCKET1_DEPTH = 3.0
POCKET2_D = 36.0
POCKET2_DEPTH = 10.0

# front tab (ear) on the left boss
TAB_Z0 = 4.2
TAB_Z1 = 11.4
TAB_LEFT_X = -20.1   # straight outer (-X) edge of the tab
TAB_TIP_R = 6.0      # round tip
TAB_TIP_Y = -33.1    # Y of the tip-arc centre
TAB_FLANK_ANG = 57.0 # direction of the straight flank (deg from +X)
TAB_BLEND_R = 14.0   # concave blend into the beam front edge
TAB_EDGE_R = 1.5     # rounding of the tab's top and bottom edges

# arc-shaped pin brackets on the top surface (concentric with a boss)
BRK_W = 10.0         # radial width of the block
BRK_PIN_D = 5.6
# boss centre x, arc radius, side (+1: right of the left boss, -1: left of the
# right boss), block angle range, pin angle range (deg), pin axis height
BRK1 = dict(cx=0.0, r=48.0, sgn=1, blk=(2.0, 22.0), pin=(-8.0, 30.0), zpin=15.0)
BRK2 = dict(cx=BOSS_DX, r=34.5, sgn=-1, blk=(-16.0, 19.0), pin=(-23.0, 26.0),
            zpin=14.2)

# handle rod with ball knob under the belly
ROD_D = 12.0
BALL_D = 17.6
# centre line: polyline corners (ball centre first) and bend radii
ROD_CORNERS = [(190.0, -1.0, -38.2), (92.0, 1.2, -27.3), (12.0, 11.0, -25.9),
               (0.5, 1.0, -25.5)]
ROD_BEND_R = [80.0, 25.0]

# clip holding the rod under the belly
CLIP_X = (87.0, 106.0)
CLIP_BW = 7.5
CLIP_Y = (-9.5, 11.5)
CLIP_Z0 = -34.6
CLIP_POCKET = (4.0, 15.0, 2.0)   # window in the underside of each clip block
CLIP_BRIDGE_Z = (-28.0, -22.0)   # bridge joining the two clip blocks
CLIP_BRIDGE_W = 12.0

# separate square tube (floating above the right boss)
TUBE_W = 31.0
TUBE_Z0 = 40.6
TUBE_H = 61.2
TUBE_FOOT = 3.5
FOOT_CHAMFER = 3.5       # smaller corner chamfer of the foot
TUBE_CHAMFER = 7.0       # 45 deg corner chamfer (leg length)
GROOVE_TOP = 7.0         # groove opening in the chamfer face
GROOVE_BOT = 4.0         # groove bottom width
GROOVE_DEPTH = 1.5

# lever mechanism on the -X face of the tube
LEV_D = 8.5
LEV_X = 163.5
# (y, z) of the top end and of the bottom end of each lever axis
LEVERS = [((2.4, 95.0), (13.0, 73.0)), ((-5.9, 75.0), (17.0, 51.0))]
STUB_D = 6.5
STUB_OUT = 5.5           # pin protrusion on the outer (-X) side of a lever


# ---------------------------------------------------------------------------
def hull_outline(wp):
    """Outline: two circles joined by their outer tangent lines."""
    d = BOSS_DX
    s = (R1 - R2) / d
    c = math.sqrt(1 - s * s)
    p1u = (R1 * s, R1 * c)
    p2u = (d + R2 * s, R2 * c)
    p1l = (R1 * s, -R1 * c)
    p2l = (d + R2 * s, -R2 * c)
    return (wp.moveTo(*p1l).lineTo(*p2l)
            .threePointArc((d + R2, 0.0), p2u)
            .lineTo(*p1u)
            .threePointArc((-R1, 0.0), p1l)
            .close())


# ---- upper plate -----------------------------------------------------------
plate = hull_outline(cq.Workplane("XY")).extrude(TOP_MAX_Z)
top_cut = (cq.Workplane("XZ").center(TOP_LOW_X, TOP_LOW_Z + TOP_ARC_R)
           .circle(TOP_ARC_R).extrude(100.0, both=True))
plate = plate.cut(top_cut)

# ---- belly -----------------------------------------------------------------
belly = hull_outline(cq.Workplane("XY")).extrude(-45.0, taper=BELLY_DRAFT)
arc_cz = BELLY_BOTTOM + BELLY_ARC_R
arc_body = (cq.Workplane("XZ").center(BELLY_ARC_CX, arc_cz)
            .circle(BELLY_ARC_R).extrude(100.0, both=True))
belly = belly.intersect(arc_body)
try:
    belly = belly.faces("<Z").edges().fillet(BELLY_FILLET)
except Exception:
    pass

body = plate.union(belly)

# ---- boss rings --------------------------------------------------------------
ring1 = cq.Workplane("XY").circle(R1).extrude(RING1_TOP)
ring2 = cq.Workplane("XY").center(BOSS_DX, 0).circle(R2).extrude(RING2_TOP)
body = body.union(ring1).union(ring2)
rec1 = (cq.Workplane("XY").workplane(offset=RING1_TOP - RECESS_DEPTH)
        .circle(RECESS_D / 2).extrude(10))
rec2 = (cq.Workplane("XY").workplane(offset=RING2_TOP - RECESS_DEPTH)
        .center(BOSS_DX, 0).circle(RECESS_D / 2).extrude(10))
body = body.cut(rec1).cut(rec2)


# ---- bottom pockets, normal to the belly arc ---------------------------------
def arc_point(x):
    dx = x - BELLY_ARC_CX
    z = arc_cz - math.sqrt(BELLY_ARC_R ** 2 - dx ** 2)
    ang = math.degrees(math.asin(dx / BELLY_ARC_R))
    return z, ang


def bottom_pocket(x, dia, depth):
    z, ang = arc_point(x)
    cyl = (cq.Workplane("XY").circle(dia / 2).extrude(depth + 20.0)
           .translate((0, 0, -20.0)))
    cyl = cyl.rotate((0, 0, 0), (0, 1, 0), -ang)  # tilt with the arc
    return cyl.translate((x, 0, z))


body = body.cut(bottom_pocket(0.0, POCKET1_D, POCKET1_DEPTH))
body = body.cut(bottom_pocket(BOSS_DX, POCKET2_D, POCKET2_DEPTH))

# ---- tab / ear on the front of the left boss ---------------------------------
def tab_solid():
    """Plan: straight outer edge, round tip, straight flank and a concave
    blend running tangentially into the front edge of the beam."""
    x0 = TAB_LEFT_X
    cx, cy = x0 + TAB_TIP_R, TAB_TIP_Y
    h0 = math.radians(TAB_FLANK_ANG)
    # end of tip arc (tangent direction = flank direction)
    phi = h0 - math.pi / 2
    C = (cx + TAB_TIP_R * math.cos(phi), cy + TAB_TIP_R * math.sin(phi))
    pm = (math.pi + (phi + 2 * math.pi)) / 2   # mid angle of the tip arc
    Mtip = (cx + TAB_TIP_R * math.cos(pm), cy + TAB_TIP_R * math.sin(pm))
    # front beam edge line (outer tangent of the two boss circles, -Y side)
    s_ = (R1 - R2) / BOSS_DX
    c_ = math.sqrt(1 - s_ * s_)
    p1 = (R1 * s_, -R1 * c_)
    p2 = (BOSS_DX + R2 * s_, -R2 * c_)
    h1 = math.atan2(p2[1] - p1[1], p2[0] - p1[0])
    m = math.tan(h1)
    rf = TAB_BLEND_R
    dx = rf * (math.sin(h0) - math.sin(h1))
    dy = rf * (-math.cos(h0) + math.cos(h1))
    ux, uy = math.cos(h0), math.sin(h0)
    # solve for flank length so that the blend ends on the beam edge
    sl = ((p1[1] + m * (C[0] + dx - p1[0])) - (C[1] + dy)) / (uy - m * ux)
    D = (C[0] + sl * ux, C[1] + sl * uy)
    E = (D[0] + dx, D[1] + dy)
    cen = (D[0] + rf * math.sin(h0), D[1] - rf * math.cos(h0))
    hm = (h0 + h1) / 2
    Mb = (cen[0] - rf * math.sin(hm), cen[1] + rf * math.cos(hm))
    prof = (cq.Workplane("XY").workplane(offset=TAB_Z0)
            .moveTo(x0, -10.0)
            .lineTo(x0, cy)
            .threePointArc(Mtip, C)
            .lineTo(*D)
            .threePointArc(Mb, E)
            .lineTo(E[0], -15.0)
            .close())
    return prof.extrude(TAB_Z1 - TAB_Z0), E


tab, tab_end = tab_solid()
try:
    tab = tab.faces(">Z or <Z").edges(cq.selectors.BoxSelector(
        (-40, -60, -10), (tab_end[0] - 0.5, -14.0, 30))).fillet(TAB_EDGE_R)
except Exception:
    pass
body = body.union(tab)


# ---- arc-shaped pin brackets ----------------------------------------------------
def bracket(cx, r, sgn, blk, pin, zpin):
    h = BRK_W / 2.0
    prof = (cq.Workplane("XZ")
            .moveTo(r - h, -2.0).lineTo(r + h, -2.0).lineTo(r + h, zpin)
            .threePointArc((r, zpin + h), (r - h, zpin)).close())
    block = prof.revolve(blk[1] - blk[0], (0, 0, 0), (0, 1, 0))
    block = block.rotate((0, 0, 0), (0, 0, 1), blk[0])
    pn = (cq.Workplane("XZ").moveTo(r, zpin).circle(BRK_PIN_D / 2)
          .revolve(pin[1] - pin[0], (0, 0, 0), (0, 1, 0)))
    pn = pn.rotate((0, 0, 0), (0, 0, 1), pin[0])
    b = block.union(pn)
    if sgn < 0:
        b = b.mirror("YZ")
    return b.translate((cx, 0, 0))


body = body.union(bracket(**BRK1)).union(bracket(**BRK2))

# ---- handle rod with ball ---------------------------------------------------------
def bent_rod(corners, radii, r):
    """Round bar following a polyline whose corners are bent with the given radii
    (cylinders joined by torus segments)."""
    P = [cq.Vector(*p) for p in corners]
    solids = []
    start = P[0]
    for i in range(1, len(P) - 1):
        u = (P[i] - P[i - 1]).normalized()
        v = (P[i + 1] - P[i]).normalized()
        th = math.acos(max(-1.0, min(1.0, u.dot(v))))
        R = radii[i - 1]
        t = R * math.tan(th / 2)
        t1 = P[i] - u * t
        t2 = P[i] + v * t
        solids.append(cq.Solid.makeCylinder(r, (t1 - start).Length, start, u))
        n = (v - u * v.dot(u)).normalized()
        c = t1 + n * R
        ax = u.cross(v).normalized()
        circ = cq.Wire.makeCircle(r, t1, u)
        solids.append(cq.Solid.revolve(circ, [], math.degrees(th), c, c + ax))
        start = t2
    u = (P[-1] - start).normalized()
    solids.append(cq.Solid.makeCylinder(r, (P[-1] - start).Length, start, u))
    res = cq.Workplane("XY").add(solids[0])
    for sld in solids[1:]:
        res = res.union(cq.Workplane("XY").add(sld))
    return res


rod = bent_rod(ROD_CORNERS, ROD_BEND_R, ROD_D / 2)
ball = cq.Workplane("XY").sphere(BALL_D / 2).translate(ROD_CORNERS[0])
rod = rod.union(ball)

# ---- clip under the belly --------------------------------------------------------
clip = None
for cx in CLIP_X:
    blk = (cq.Workplane("XY").box(CLIP_BW, CLIP_Y[1] - CLIP_Y[0], 14.0,
                                  centered=(True, False, False))
           .translate((cx, CLIP_Y[0], CLIP_Z0)))
    win = (cq.Workplane("XY").box(CLIP_POCKET[0], CLIP_POCKET[1], CLIP_POCKET[2],
                                  centered=(True, True, False))
           .translate((cx, (CLIP_Y[0] + CLIP_Y[1]) / 2, CLIP_Z0)))
    blk = blk.cut(win)
    clip = blk if clip is None else clip.union(blk)
bridge = (cq.Workplane("XY").box(CLIP_X[1] - CLIP_X[0], CLIP_BRIDGE_W,
                                 CLIP_BRIDGE_Z[1] - CLIP_BRIDGE_Z[0],
                                 centered=(True, True, False))
          .translate(((CLIP_X[0] + CLIP_X[1]) / 2, (CLIP_Y[0] + CLIP_Y[1]) / 2,
                      CLIP_BRIDGE_Z[0])))
clip = clip.union(bridge)

body = body.union(clip).union(rod)

# ---- square tube (separate body) -------------------------------------------------
h = TUBE_W / 2.0
c = TUBE_CHAMFER
# octagonal section (square with 45 deg chamfered corners) with a trapezoidal
# groove in every chamfer face
sec = []
corners = [(1, 1), (-1, 1), (-1, -1), (1, -1)]
for sx, sy in corners:
    # chamfer from the side face x=sx*h to the side face y=sy*h
    a = (sx * h, sy * (h - c))
    b = (sx * (h - c), sy * h)
    mx, my = (a[0] + b[0]) / 2, (a[1] + b[1]) / 2
    tx, ty = (b[0] - a[0]) / (c * math.sqrt(2)), (b[1] - a[1]) / (c * math.sqrt(2))
    nx, ny = -sx / math.sqrt(2), -sy / math.sqrt(2)   # inward normal
    g1 = (mx - tx * GROOVE_TOP / 2, my - ty * GROOVE_TOP / 2)
    g2 = (mx - tx * GROOVE_BOT / 2 + nx * GROOVE_DEPTH,
          my - ty * GROOVE_BOT / 2 + ny * GROOVE_DEPTH)
    g3 = (mx + tx * GROOVE_BOT / 2 + nx * GROOVE_DEPTH,
          my + ty * GROOVE_BOT / 2 + ny * GROOVE_DEPTH)
    g4 = (mx + tx * GROOVE_TOP / 2, my + ty * GROOVE_TOP / 2)
    sec += [a, g1, g2, g3, g4, b]
# corners are listed counter-clockwise; inside each corner the points run from
# the x-face to the y-face, so every second corner is reversed to keep the
# outline continuous
pts2 = []
for i, (sx, sy) in enumerate(corners):
    seg = sec[i * 6:(i + 1) * 6]
    if sx * sy < 0:
        seg = seg[::-1]
    pts2 += seg
shaft = (cq.Workplane("XY").workplane(offset=TUBE_Z0 + TUBE_FOOT)
         .polyline(pts2).close().extrude(TUBE_H - TUBE_FOOT))
foot = (cq.Workplane("XY").workplane(offset=TUBE_Z0)
        .rect(TUBE_W, TUBE_W).extrude(TUBE_FOOT)
        .edges("|Z").chamfer(FOOT_CHAMFER))
tube = shaft.union(foot).translate((BOSS_DX, 0, 0))

# levers on the -X side of the tube
for (ya, za), (yb, zb) in LEVERS:
    a = cq.Vector(LEV_X, ya, za)
    bvec = cq.Vector(LEV_X, yb, zb)
    axis = (bvec - a)
    L = axis.Length
    pl = cq.Plane(origin=a, xDir=cq.Vector(1, 0, 0), normal=axis.normalized())
    lev = cq.Workplane(pl).circle(LEV_D / 2).extrude(L)
    sp = a + axis.normalized() * 3.5
    stub = (cq.Workplane("YZ").workplane(offset=LEV_X - STUB_OUT).center(sp.y, sp.z)
            .circle(STUB_D / 2).extrude(BOSS_DX - h - LEV_X + STUB_OUT + 1.0))
    tube = tube.union(lev).union(stub)

result = body.union(tube)
